import cadquery as cq
import math

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
HEX_R = 480.0          # hexagon circumradius (vertices on +/-X)
PLATE_T = 1.5          # plate thickness
CENTER_HOLE_D = 30.0

TRI_SIDE = 230.0       # equilateral triangular windows (all pointing +Y)
TRI_CENTROID_R = 272.0
TRI_ANGLES = (270.0, 30.0, 150.0)

SLOT_W = 18.0
SLOT_X0, SLOT_X1 = 25.0, 137.0   # slot extent along its axis (first slot along +X)
SLOT_OFF = -7.6                  # lateral offset of slot centreline

# motor + bracket placement (first unit: shaft pointing -X), 3 units at 120 deg
MOTOR_FRONT_X = 15.0   # x of bracket front face
MOTOR_AXIS_Y = -64.0
MOTOR_AXIS_Z = 38.0    # axis height above plate top

# L bracket
BR_W = 70.0
BR_T = 5.0
BR_H = 71.0
BR_TOP_CH = 6.0
BR_FOOT_L = 72.0
BR_FOOT_T = 5.0
BR_BORE_D = 40.0
BR_SLOT_W = 6.0
BR_SLOT_Y = 21.0
BR_SLOT_X0, BR_SLOT_X1 = 16.0, 62.0
GUSSET_H = 20.0
GUSSET_L = 15.0

# motor (60 frame)
M_SQ = 60.0            # flange / end cap square
BODY_SQ = 56.0         # housing square
FLANGE_T = 8.0
BODY_L = 98.0
BODY_R = 9.0           # rounded housing corners (expose flange bolt heads)
CAP_L = 15.0
STEP = 5.0             # corner step size on the end cap
HUMP_H = 9.0
HUMP_W_TOP = 26.0
PILOT_D = 36.0
HUB_D = 20.0
SHAFT_D = 12.0
SHAFT_L = 25.0         # from bracket front face
MOUNT_PITCH = 50.0
MOUNT_HOLE_D = 5.0

# thin flat cable strip lying under the plate (runs to the +Y edge)
STRIP_T = 0.5
STRIP_X0, STRIP_X1 = -81.0, -59.0
STRIP_Y0 = 45.0


def stepped_square(c, s, hump=0.0, hump_top=0.0):
    """(y,z) outline of a square of half-size c with two-step notched corners,
    optionally with a stepped hump (connector housing) on top."""
    pts = [(c, -c + 2 * s), (c, c - 2 * s), (c - s, c - 2 * s), (c - s, c - s),
           (c - 2 * s, c - s), (c - 2 * s, c)]
    if hump > 0:
        hw = hump_top / 2
        hm = (hw + c - 2 * s) / 2
        pts += [(hm, c), (hm, c + hump / 2), (hw, c + hump / 2), (hw, c + hump),
                (-hw, c + hump), (-hw, c + hump / 2), (-hm, c + hump / 2), (-hm, c)]
    pts += [(-c + 2 * s, c), (-c + 2 * s, c - s), (-c + s, c - s), (-c + s, c - 2 * s),
            (-c, c - 2 * s), (-c, -c + 2 * s), (-c + s, -c + 2 * s), (-c + s, -c + s),
            (-c + 2 * s, -c + s), (-c + 2 * s, -c), (c - 2 * s, -c), (c - 2 * s, -c + s),
            (c - s, -c + s), (c - s, -c + 2 * s)]
    return pts


def motor_unit():
    """Motor + L bracket in local frame: axis = X axis, shaft toward -X,
    bracket front face at x=0, plate top at z=-MOTOR_AXIS_Z."""
    zb = -MOTOR_AXIS_Z  # base (plate top) level in local frame
    mp = [(sy * MOUNT_PITCH / 2, sz * MOUNT_PITCH / 2) for sy in (-1, 1) for sz in (-1, 1)]

    # ---- bracket vertical plate ----
    vp = (cq.Workplane("YZ").center(0, zb + BR_H / 2).rect(BR_W, BR_H).extrude(BR_T))
    vp = vp.edges("|X and >Z").chamfer(BR_TOP_CH)
    vp = vp.cut(cq.Workplane("YZ").circle(BR_BORE_D / 2).extrude(BR_T))
    vp = vp.cut(cq.Workplane("YZ").pushPoints(mp).circle(MOUNT_HOLE_D / 2).extrude(BR_T))

    # ---- foot ----
    foot = (cq.Workplane("XY").workplane(offset=zb)
            .center(BR_FOOT_L / 2, 0).rect(BR_FOOT_L, BR_W).extrude(BR_FOOT_T))
    foot = foot.edges("|Z and >X").chamfer(5.0)
    for sy in (-1, 1):
        sl = (cq.Workplane("XY").workplane(offset=zb)
              .center((BR_SLOT_X0 + BR_SLOT_X1) / 2, sy * BR_SLOT_Y)
              .slot2D(BR_SLOT_X1 - BR_SLOT_X0, BR_SLOT_W).extrude(BR_FOOT_T))
        foot = foot.cut(sl)
    br = vp.union(foot)

    # ---- side gussets ----
    for sy in (-1, 1):
        yc = sy * (BR_W / 2 - BR_T / 2)
        g = (cq.Workplane("XZ", origin=(0, yc + BR_T / 2, 0))
             .polyline([(BR_T, zb + BR_FOOT_T), (BR_T + GUSSET_L, zb + BR_FOOT_T),
                        (BR_T, zb + BR_FOOT_T + GUSSET_H)]).close().extrude(BR_T))
        br = br.union(g)

    # ---- motor ----
    c = M_SQ / 2
    x = BR_T
    fl = (cq.Workplane("YZ").workplane(offset=x).rect(M_SQ, M_SQ).extrude(FLANGE_T)
          .edges("|X").chamfer(2.0))
    fl = fl.cut(cq.Workplane("YZ").workplane(offset=x).pushPoints(mp)
                .circle(MOUNT_HOLE_D / 2).extrude(FLANGE_T))
    pilot = cq.Workplane("YZ").workplane(offset=x).circle(PILOT_D / 2).extrude(-3.0)
    pilot = pilot.cut(cq.Workplane("YZ").workplane(offset=x - 3.0)
                      .circle(PILOT_D / 2 - 4).circle(HUB_D / 2).extrude(1.5))
    x += FLANGE_T
    body = (cq.Workplane("YZ").workplane(offset=x).rect(BODY_SQ, BODY_SQ)
            .extrude(BODY_L).edges("|X").fillet(BODY_R))
    x += BODY_L
    cap = (cq.Workplane("YZ").workplane(offset=x)
           .polyline(stepped_square(c, STEP, HUMP_H, HUMP_W_TOP)).close().extrude(CAP_L))
    shaft = (cq.Workplane("YZ").workplane(offset=BR_T - 3.0)
             .circle(SHAFT_D / 2).extrude(-(SHAFT_L + BR_T - 3.0)))
    shaft = shaft.faces("<X").chamfer(0.8)

    m = fl.union(pilot).union(body).union(cap).union(shaft)
    return br.union(m)


# ---------------- plate ----------------
plate = cq.Workplane("XY").polygon(6, 2 * HEX_R).extrude(PLATE_T)
plate = plate.cut(cq.Workplane("XY").circle(CENTER_HOLE_D / 2).extrude(PLATE_T))

h_tri = TRI_SIDE * math.sqrt(3) / 2
for a in TRI_ANGLES:
    cx = TRI_CENTROID_R * math.cos(math.radians(a))
    cy = TRI_CENTROID_R * math.sin(math.radians(a))
    tri = [(cx, cy + 2 * h_tri / 3), (cx - TRI_SIDE / 2, cy - h_tri / 3),
           (cx + TRI_SIDE / 2, cy - h_tri / 3)]
    plate = plate.cut(cq.Workplane("XY").polyline(tri).close().extrude(PLATE_T))

slot_len = SLOT_X1 - SLOT_X0
for k in range(3):
    ang = 120.0 * k
    s = (cq.Workplane("XY").center((SLOT_X0 + SLOT_X1) / 2, SLOT_OFF)
         .slot2D(slot_len, SLOT_W).extrude(PLATE_T)
         .rotate((0, 0, 0), (0, 0, 1), ang))
    plate = plate.cut(s)
    # screw holes under the bracket foot slots
    hp = [(MOTOR_FRONT_X + xx, MOTOR_AXIS_Y + sy * BR_SLOT_Y)
          for xx in (BR_SLOT_X0 + 4, BR_SLOT_X1 - 4) for sy in (-1, 1)]
    hs = (cq.Workplane("XY").pushPoints(hp).circle(2.5).extrude(PLATE_T)
          .rotate((0, 0, 0), (0, 0, 1), ang))
    plate = plate.cut(hs)

# flat cable strip under the plate: straight band to the +Y edge with a folded end
edge_y = HEX_R * math.sqrt(3) / 2
strip_pts = [(STRIP_X0, edge_y), (STRIP_X0, STRIP_Y0), (-100.0, 20.0), (-42.0, 5.0),
             (-38.5, 62.0), (STRIP_X1, 80.0), (STRIP_X1, edge_y)]
fold_pts = [(-100.0, 20.0), (-42.0, 5.0), (-38.5, 62.0), (-84.0, 18.0)]
strip = (cq.Workplane("XY").workplane(offset=-STRIP_T)
         .polyline(strip_pts).close().extrude(STRIP_T))
fold = (cq.Workplane("XY").workplane(offset=-2 * STRIP_T)
        .polyline(fold_pts).close().extrude(STRIP_T))
plate = plate.union(strip).union(fold)

unit = motor_unit().translate((MOTOR_FRONT_X, MOTOR_AXIS_Y, PLATE_T + MOTOR_AXIS_Z))
result = plate
for k in range(3):
    result = result.union(unit.rotate((0, 0, 0), (0, 0, 1), 120.0 * k))
